"""NFC / RFID reader mounting plate.

A flat rounded-rectangle plate: top face carries an engraved "wireless"
symbol (dot + three pairs of concentric arc grooves), a row of three
chamfered through holes and four countersunk corner screw holes.  The
underside is hollowed into a shallow tray (deep pocket leaving a thin
perimeter lip) with four short screw bosses hanging from the pocket floor.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 165.0            # plate length (X)
W = 105.0            # plate width (Y)
T = 8.0              # overall height (Z), lip included
R_CORNER = 8.0       # vertical corner radius (plan view)
R_TOP = 2.0          # top outer edge fillet

# underside pocket (leaves a narrow lip around the perimeter)
LIP = 2.0            # lip wall thickness
POCKET_D = 4.4       # pocket depth -> top skin = T - POCKET_D

# countersunk corner holes
HOLE_INSET_X = 10.8
HOLE_INSET_Y = 10.6
CSK_HOLE_D = 3.6
CSK_D = 6.9
CSK_ANGLE = 90.0

# row of three chamfered through holes
ROW_Y = 11.6
ROW_PITCH = 17.4
ROW_HOLE_D = 4.8
ROW_CHAMF = 0.4

# engraved wireless symbol
SYM_X = 0.0
SYM_Y = -22.2
DOT_D = 6.5
ENGRAVE_D = 1.1
ARC_W = 1.8
ARC_RADII = [12.45, 21.8, 31.0]
ARC_HALF_ANG = [46.0, 42.0, 40.5]   # half sweep, measured to the end-cap centres

# screw bosses hanging from the pocket floor
BOSS_X = 38.0
BOSS_Y = [-45.3, 3.6]
BOSS_D = 5.7
BOSS_H = 1.7
BOSS_HOLE_D = 3.4
BOSS_HOLE_DEPTH = 4.3

# ---------------- base plate ----------------
plate = (
    cq.Workplane("XY")
    .box(L, W, T, centered=(True, True, False))
    .edges("|Z").fillet(R_CORNER)
    .faces(">Z").edges().fillet(R_TOP)
)

# underside pocket -> thin-walled tray with a perimeter lip
pocket = (
    cq.Workplane("XY")
    .rect(L - 2 * LIP, W - 2 * LIP)
    .extrude(POCKET_D)
    .edges("|Z").fillet(R_CORNER - LIP)
)
plate = plate.cut(pocket)
z_floor = POCKET_D

# ---------------- screw bosses on the pocket floor ----------------
boss_pts = [(sx * BOSS_X, by) for by in BOSS_Y for sx in (-1, 1)]
bosses = (
    cq.Workplane("XY").workplane(offset=z_floor - BOSS_H)
    .pushPoints(boss_pts).circle(BOSS_D / 2.0).extrude(BOSS_H + 0.5)
)
plate = plate.union(bosses)
boss_holes = (
    cq.Workplane("XY").workplane(offset=z_floor - BOSS_H - 0.5)
    .pushPoints(boss_pts).circle(BOSS_HOLE_D / 2.0)
    .extrude(BOSS_HOLE_DEPTH + 0.5)
)
plate = plate.cut(boss_holes)


# ---------------- countersunk / chamfered through holes ----------------
def csk_cutter(x, y, d, dk, ang, top):
    """Through hole of diameter d with a conical countersink of top diameter dk."""
    h = (dk - d) / 2.0 / math.tan(math.radians(ang / 2.0))
    cyl = cq.Solid.makeCylinder(d / 2.0, top + 2.0, cq.Vector(x, y, -1.0))
    cone = cq.Solid.makeCone(dk / 2.0, d / 2.0, h,
                             cq.Vector(x, y, top), cq.Vector(0, 0, -1))
    cap = cq.Solid.makeCylinder(dk / 2.0, 1.0, cq.Vector(x, y, top))
    return cyl.fuse(cone).fuse(cap)


corner_pts = [(sx * (L / 2 - HOLE_INSET_X), sy * (W / 2 - HOLE_INSET_Y))
              for sx in (-1, 1) for sy in (-1, 1)]
for (x, y) in corner_pts:
    plate = plate.cut(cq.Workplane().add(
        csk_cutter(x, y, CSK_HOLE_D, CSK_D, CSK_ANGLE, T)))

for i in (-1, 0, 1):
    plate = plate.cut(cq.Workplane().add(
        csk_cutter(i * ROW_PITCH, ROW_Y, ROW_HOLE_D,
                   ROW_HOLE_D + 2 * ROW_CHAMF, 90.0, T)))

# ---------------- engraved wireless symbol ----------------
dot = (cq.Workplane("XY").workplane(offset=T - ENGRAVE_D)
       .center(SYM_X, SYM_Y).circle(DOT_D / 2.0).extrude(ENGRAVE_D + 1.0))
plate = plate.cut(dot)


def arc_slot(cx, cy, r, w, half_ang, side):
    """Round-ended arc groove centred on angle 0 (side=+1) or 180 deg (side=-1)."""
    a = math.radians(half_ang)
    ro, ri, hw = r + w / 2.0, r - w / 2.0, w / 2.0

    def P(rad, th):
        return (cx + side * rad * math.cos(th), cy + rad * math.sin(th))

    cap_top = (cx + side * (r * math.cos(a) - hw * math.sin(a)),
               cy + r * math.sin(a) + hw * math.cos(a))
    cap_bot = (cx + side * (r * math.cos(a) - hw * math.sin(a)),
               cy - r * math.sin(a) - hw * math.cos(a))
    prof = (cq.Workplane("XY").workplane(offset=T - ENGRAVE_D)
            .moveTo(*P(ro, -a))
            .threePointArc(P(ro, 0.0), P(ro, a))
            .threePointArc(cap_top, P(ri, a))
            .threePointArc(P(ri, 0.0), P(ri, -a))
            .threePointArc(cap_bot, P(ro, -a))
            .close())
    return prof.extrude(ENGRAVE_D + 1.0)


for r, ha in zip(ARC_RADII, ARC_HALF_ANG):
    for side in (-1, 1):
        plate = plate.cut(arc_slot(SYM_X, SYM_Y, r, ARC_W, ha, side))

result = plate

VIEW = {"azimuth": 45, "elevation": 26}
